import cadquery as cq
from OCP.BRepClass3d import BRepClass3d_SolidClassifier
from OCP.TopAbs import TopAbs_IN
from OCP.gp import gp_Pnt

# ---------------- driving dimensions (mm) ----------------
T_WALL = 3.3          # wall thickness
H_TOP = 34.5          # top of the ordinary walls
H_RAISED = 44.0       # top of the raised right-hand walls
Z_FLOOR_BOT = 20.0    # underside of the tray floor (outer seam line)
Z_FLOOR_TOP = 22.2    # top of the tray floor
TOP_FILLET = 1.0      # rounding of the wall tops
# sloped underside plane  z = BOT_C - BOT_AX * x - BOT_AY * y
BOT_C = 21.25
BOT_AX = 0.080
BOT_AY = 0.042

LENGTH = 200.0        # overall X size
X_LEFT_END = 82.0     # right end of the left (rectangular) section
Y_LEFT_FRONT = 42.5   # front face of the left section
Y_BACK = 130.6        # back face of the left section / right-back segment
# stepped back wall: (x_start, x_end, y_back) of the middle segments
BACK_STEPS = [
    (54.9, X_LEFT_END, 137.2),
    (X_LEFT_END, 115.5, 140.6),
    (115.5, 142.7, 137.2),
    (142.7, 170.4, 134.4),
]
X_RAISE = 170.4       # raised walls start here (back wall) ...
Y_RAISE = 39.0        # ... and at the front right corner E (right wall)
# chamfered front of the right section
P_B = (97.8, 21.6)
P_C = (152.0, 14.0)
P_D = (177.1, 0.0)

# outline of the part (plan view), counter-clockwise
OUTLINE = [
    (0.0, Y_LEFT_FRONT),
    (X_LEFT_END, Y_LEFT_FRONT),
    P_B,
    P_C,
    P_D,
    (LENGTH, Y_RAISE),
    (LENGTH, Y_BACK),
    (BACK_STEPS[-1][1], Y_BACK),
]
for (xs, xe, yb) in reversed(BACK_STEPS):
    OUTLINE += [(xe, yb), (xs, yb)]
OUTLINE += [(BACK_STEPS[0][0], Y_BACK), (0.0, Y_BACK)]

# small holes in the tray floor
FLOOR_HOLES = [(30.4, 100.2), (30.4, 73.3), (92.5, 48.3), (139.5, 105.8), (159.3, 36.6)]
FLOOR_HOLE_D = 3.2

# big side holes
SIDE_HOLE_D = 13.9
SIDE_HOLE_Y = 57.9     # on the right (x max) wall
SIDE_HOLE_Z = 27.6
BACK_HOLE_W = 18.5     # slot in the raised back wall segment: overall width ...
BACK_HOLE_D = 13.9     # ... and height
BACK_HOLE_X = 183.5
BACK_HOLE_Z = 28.3


def poly_wire(pts):
    return cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True)


def prism(wire, z0, z1):
    face = cq.Face.makeFromWires(wire.moved(cq.Location(cq.Vector(0, 0, z0))))
    return cq.Solid.extrudeLinear(face, cq.Vector(0, 0, z1 - z0))


def wp(shape):
    return cq.Workplane("XY").add(shape)


outer_w = poly_wire(OUTLINE)
inner_w = outer_w.offset2D(-T_WALL, "intersection")[0]

Z_LOW = -10.0

# the raised right wall ends on the mitre line through the outer corner E and
# the matching inner corner
_inner_pts = [v.toTuple() for v in inner_w.Vertices()]
_E_IN = min((p for p in _inner_pts if abs(p[0] - (LENGTH - T_WALL)) < 1e-6), key=lambda p: p[1])
_E_OUT = (LENGTH, Y_RAISE)
_dx, _dy = _E_IN[0] - _E_OUT[0], _E_IN[1] - _E_OUT[1]
RAISE_REGION = [
    (_E_OUT[0] - 3 * _dx, _E_OUT[1] - 3 * _dy),
    (_E_OUT[0] + 3 * _dx, _E_OUT[1] + 3 * _dy),
    (_E_OUT[0] + 3 * _dx, 120.0),
    (X_RAISE, 120.0),
    (X_RAISE, 160.0),
    (_E_OUT[0] - 3 * _dx, 160.0),
]

# ---------- upper part: tray walls + floor (above the seam) ----------
tray = wp(prism(outer_w, Z_FLOOR_BOT, H_TOP)).cut(wp(prism(inner_w, Z_FLOOR_TOP, H_TOP + 1)))

# raised walls on the right / back-right
ring = wp(prism(outer_w, H_TOP, H_RAISED)).cut(wp(prism(inner_w, H_TOP - 1, H_RAISED + 1)))
raise_box = wp(prism(poly_wire(RAISE_REGION), H_TOP - 5, H_RAISED + 5))
upper = tray.union(ring.intersect(raise_box))

# floor holes
for (hx, hy) in FLOOR_HOLES:
    upper = upper.cut(
        cq.Workplane("XY").workplane(offset=Z_FLOOR_BOT - 1).center(hx, hy)
        .circle(FLOOR_HOLE_D / 2).extrude(Z_FLOOR_TOP - Z_FLOOR_BOT + 2)
    )

# big side holes: round, flattened at the floor level (flush with the floor top)
def d_hole(d, length, base, direction):
    cyl = wp(cq.Solid.makeCylinder(d / 2, length, base, direction))
    keep = cq.Workplane("XY").box(400, 400, 100, centered=(True, True, False)).translate((100, 70, Z_FLOOR_TOP))
    return cyl.intersect(keep)


# hole in the right (x max) wall, axis along X
upper = upper.cut(d_hole(SIDE_HOLE_D, 3 * T_WALL,
                         cq.Vector(LENGTH - 2 * T_WALL, SIDE_HOLE_Y, SIDE_HOLE_Z), cq.Vector(1, 0, 0)))
# horizontally elongated hole (slot) in the raised back wall segment, axis along Y
back_slot = (
    cq.Workplane(cq.Plane(origin=(BACK_HOLE_X, Y_BACK - 2 * T_WALL, BACK_HOLE_Z),
                          xDir=(1, 0, 0), normal=(0, 1, 0)))
    .slot2D(BACK_HOLE_W, BACK_HOLE_D)
    .extrude(3 * T_WALL)
)
floor_keep = cq.Workplane("XY").box(400, 400, 100, centered=(True, True, False)).translate((100, 70, Z_FLOOR_TOP))
upper = upper.cut(back_slot.intersect(floor_keep))

# round the convex top edges of the walls
up_solid = upper.val()


def _is_top_convex(edge):
    b = edge.BoundingBox()
    if b.zlen > 1e-3:
        return False
    z = b.zmin
    if abs(z - H_TOP) > 1e-3 and abs(z - H_RAISED) > 1e-3:
        return False
    if edge.geomType() != "LINE":
        return False
    # convexity test: a probe offset along (n1 - n2) lies outside for convex edges only
    mid = edge.positionAt(0.5)
    faces = [f for f in up_solid.Faces() if any(e.isSame(edge) for e in f.Edges())]
    if len(faces) != 2:
        return False
    n1 = faces[0].normalAt(mid)
    n2 = faces[1].normalAt(mid)
    p = mid + (n1 - n2) * 0.05
    cls = BRepClass3d_SolidClassifier(up_solid.wrapped, gp_Pnt(p.x, p.y, p.z), 1e-6)
    return cls.State() != TopAbs_IN


top_edges = [e for e in up_solid.Edges() if _is_top_convex(e)]
if TOP_FILLET > 0 and top_edges:
    try:
        up_solid = up_solid.fillet(TOP_FILLET, top_edges)
    except Exception:
        pass

# ---------- lower part: skirt below the floor, cut by the sloped underside ----------
skirt = wp(prism(outer_w, Z_LOW, Z_FLOOR_BOT)).cut(wp(prism(inner_w, Z_LOW - 1, Z_FLOOR_BOT + 0.0)))
n = cq.Vector(BOT_AX, BOT_AY, 1.0).normalized()
cutter = (
    cq.Workplane(cq.Plane(origin=cq.Vector(0, 0, BOT_C),
                          xDir=cq.Vector(1, 0, -BOT_AX).normalized(), normal=n))
    .rect(800, 800)
    .extrude(-100)
)
skirt = skirt.cut(cutter)

# join without merging coplanar faces, so the seam line at the floor level stays
body = up_solid.fuse(skirt.val())

_solids = body.Solids()
result = _solids[0] if len(_solids) == 1 else body

VIEW = {"azimuth": 45, "elevation": 26}
